import math
import cadquery as cq
from cadquery.func import loft

# ---------------------------------------------------------------------------
# Small wind-turbine style blade: cylindrical root, blended root transition
# and a tapered airfoil blade.
#   Z  : span axis (tip at z = 0, flat root face at z = SPAN)
#   X  : chord direction (leading edge toward -X, trailing edge toward +X)
#   Y  : thickness direction (suction side toward +Y)
# The body is one smooth loft through a handful of spanwise stations whose
# chord / thickness / shape are driven by the parameters below.
# ---------------------------------------------------------------------------

SPAN = 300.0            # overall length, tip to root face
ROOT_R = 10.0           # root cylinder radius
ROOT_STRAIGHT = 10.0    # straight cylindrical length at the root
TRANS_END = 222.0       # z where the pure airfoil starts (max chord region)

LE_TIP, LE_MAX = -2.0, -10.5                  # leading edge x at z=0 and z=TRANS_END
LE_EXP = 1.2                                  # leading edge curvature along span
TE_TIP, TE_SLOPE = 4.9, 0.0765                # trailing edge x = TE_TIP + slope*z
TE_MAX = 21.3                                 # trailing edge x at the max chord
T_MAXCHORD = 8.1                              # thickness at the max chord station
TC_TIP = 0.10                                 # thickness / chord at the tip
TC_EXP = 1.85                                 # spanwise growth of thickness ratio
CAMBER = 0.02                                 # NACA style max camber / chord
CAMBER_POS = 0.4                              # chordwise position of max camber
PREBEND = 0.6                                 # +Y offset of the tip section
PREBEND_Z = 170.0                             # span over which the prebend acts
TIP_R_TE = 4.5                                # tip rounding radius, trailing corner
TIP_R_LE = 1.0                                # tip rounding radius, leading corner
N_PTS = 14                                    # spline points per airfoil side
LOFT_PARAM = "centripetal"                    # loft section parametrization

# spanwise stations (z) of the loft: denser through the root transition,
# coarser along the straight taper of the outer blade
STATION_Z = [SPAN - ROOT_STRAIGHT,
             283.0, 276.0, 268.0, 259.0, 249.0, 237.0, TRANS_END,
             200.0, 168.0, 122.0, 65.0, 0.0]

# root transition table  z : (trailing edge x, thickness, ellipse blend)
#   the section turns from the root circle into a thick sharp-edged airfoil
TRANSITION = [
    (SPAN - ROOT_STRAIGHT, ROOT_R, 2 * ROOT_R, 1.0),
    (283.0, 10.0, 19.2, 1.0),
    (276.0, 10.1, 17.6, 0.7),
    (268.0, 11.8, 15.5, 0.2),
    (259.0, 14.7, 13.6, 0.08),
    (249.0, 17.9, 11.7, 0.0),
    (237.0, 20.5, 10.0, 0.0),
    (TRANS_END, TE_MAX, T_MAXCHORD, 0.0),
]


def _lerp_table(z, col):
    t = TRANSITION
    for (z0, *a), (z1, *b) in zip(t, t[1:]):
        if z1 <= z <= z0:
            s = (z - z1) / (z0 - z1)
            return b[col] + s * (a[col] - b[col])
    raise ValueError(z)


def leading_edge(z):
    if z >= TRANS_END:
        # blend from the max-chord leading edge back onto the cylinder
        s = min(1.0, (z - TRANS_END) / (SPAN - ROOT_STRAIGHT - TRANS_END))
        return LE_MAX + (-ROOT_R - LE_MAX) * s * s
    # gently curved leading edge line from the tip to the max chord
    return LE_TIP + (LE_MAX - LE_TIP) * (z / TRANS_END) ** LE_EXP


def station(z):
    """(z, x_le, x_te, thickness, blend) for a spanwise position."""
    if z >= SPAN - ROOT_STRAIGHT:
        return (z, -ROOT_R, ROOT_R, 2 * ROOT_R, 1.0)
    x_le = leading_edge(z)
    if z >= TRANS_END:
        x_te = _lerp_table(z, 0)
        thick = _lerp_table(z, 1)
        blend = _lerp_table(z, 2)
    else:
        x_te = min(TE_TIP + TE_SLOPE * z, TE_MAX)
        chord = x_te - x_le
        # thickness ratio grows from TC_TIP at the tip to the max-chord value
        tc_root = T_MAXCHORD / (TE_MAX - LE_MAX)
        tc = TC_TIP + (tc_root - TC_TIP) * (z / TRANS_END) ** TC_EXP
        thick = tc * chord
        blend = 0.0
    return (z, x_le, x_te, thick, blend)


def _naca_half(x):
    """NACA 4-digit half thickness for unit thickness (closed trailing edge)."""
    return 5.0 * (0.2969 * math.sqrt(x) - 0.1260 * x - 0.3516 * x ** 2
                  + 0.2843 * x ** 3 - 0.1036 * x ** 4)


def _camber(x, m, p):
    if m == 0.0:
        return 0.0
    if x < p:
        return m / p ** 2 * (2 * p * x - x * x)
    return m / (1 - p) ** 2 * ((1 - 2 * p) + 2 * p * x - x * x)


def _spline_params():
    """Common spline parameters for every section (chord-length spacing of a
    reference 20 % airfoil) so all sections share one knot vector."""
    pts = []
    for i in range(N_PTS + 1):
        xo = 0.5 * (1.0 + math.cos(math.pi * i / N_PTS))
        pts.append((xo, 0.2 * _naca_half(min(max(xo, 0.0), 1.0))))
    acc = [0.0]
    for (x0, y0), (x1, y1) in zip(pts, pts[1:]):
        acc.append(acc[-1] + math.hypot(x1 - x0, y1 - y0))
    return [a / acc[-1] for a in acc]


SPLINE_PARAMS = _spline_params()


def section_wire(z, x_le, x_te, thick, blend):
    """Closed section: upper spline TE->LE, lower spline LE->TE.
    blend=1 gives an ellipse (a circle when chord == thickness), blend=0 a
    cambered NACA-style airfoil with a sharp trailing edge."""
    chord = x_te - x_le
    m = CAMBER * (1.0 - blend)
    dy = PREBEND * max(0.0, 1.0 - z / PREBEND_Z) ** 2
    upper, lower = [], []
    for i in range(N_PTS + 1):
        u = i / N_PTS                       # 0 -> TE, 1 -> LE
        xo = min(max(0.5 * (1.0 + math.cos(math.pi * u)), 0.0), 1.0)
        ell = math.sqrt(max(xo * (1.0 - xo), 0.0))
        yt = thick * (blend * ell + (1.0 - blend) * _naca_half(xo))
        yc = chord * _camber(xo, m, CAMBER_POS)
        x = x_le + chord * xo
        upper.append(cq.Vector(x, dy + yc + yt, z))
        lower.append(cq.Vector(x, dy + yc - yt, z))
    lower.reverse()
    p_up = SPLINE_PARAMS
    p_lo = [1.0 - p for p in reversed(SPLINE_PARAMS)]
    e_up = cq.Edge.makeSpline(upper, parameters=p_up, scale=False)
    e_lo = cq.Edge.makeSpline(lower, parameters=p_lo, scale=False)
    return cq.Wire.assembleEdges([e_up, e_lo])


def corner_cutter(p0, d1, d2, r, depth=12.0, margin=2.0):
    """Prism (along Y) that rounds the planform corner p0 (x, z) formed by the
    edge directions d1, d2 (pointing away from the corner) with radius r."""
    def unit(v):
        n = math.hypot(*v)
        return (v[0] / n, v[1] / n)

    d1, d2 = unit(d1), unit(d2)
    half = math.acos(max(-1.0, min(1.0, d1[0] * d2[0] + d1[1] * d2[1]))) / 2.0
    bis = unit((d1[0] + d2[0], d1[1] + d2[1]))
    t = r / math.tan(half)
    c = (p0[0] + bis[0] * r / math.sin(half), p0[1] + bis[1] * r / math.sin(half))
    t1 = (p0[0] + d1[0] * t, p0[1] + d1[1] * t)
    t2 = (p0[0] + d2[0] * t, p0[1] + d2[1] * t)
    mid = (c[0] - bis[0] * r, c[1] - bis[1] * r)

    def out(p):   # push a tangent point outward, away from the arc centre
        v = unit((p[0] - c[0], p[1] - c[1]))
        return (p[0] + v[0] * margin, p[1] + v[1] * margin)

    corner = (p0[0] - bis[0] * margin * 2, p0[1] - bis[1] * margin * 2)
    return (cq.Workplane("XZ")
            .moveTo(*t1).lineTo(*out(t1)).lineTo(*corner).lineTo(*out(t2))
            .lineTo(*t2).threePointArc(mid, t1).close()
            .extrude(depth, both=True))


STATIONS = [station(z) for z in STATION_Z]
wires = [section_wire(*s) for s in STATIONS]

# blade: one smooth loft from the end of the root cylinder down to the tip
blade = loft(wires, cap=True, ruled=False, parametrization=LOFT_PARAM, degree=3)

# root: straight cylinder extruded from the very same circular section
root = cq.Solid.extrudeLinear(cq.Face.makeFromWires(wires[0]),
                              cq.Vector(0, 0, ROOT_STRAIGHT))

body = cq.Workplane("XY").add(blade.fuse(root).clean())

# rounded tip: round both planform corners of the flat tip face
le_slope = (leading_edge(10.0) - LE_TIP) / 10.0
tip_te = corner_cutter((TE_TIP, 0.0), (-1.0, 0.0), (TE_SLOPE, 1.0), TIP_R_TE)
tip_le = corner_cutter((LE_TIP, 0.0), (1.0, 0.0), (le_slope, 1.0), TIP_R_LE)
result = body.cut(tip_te).cut(tip_le)

VIEW = {"azimuth": 45, "elevation": 26}
